"""Dome cap: base ring, hemispherical shell with a top opening and four box-cut side
windows (leaving four diagonal legs), a flat cross bar across the bottom opening and two
diametrically opposed snap clips (root block + chamfered cantilever arm) inside the ring."""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R = 50.0            # outer radius of base ring and dome sphere
H_RING = 16.2       # base ring height (= height of the dome sphere centre)
WIN_SILL = 15.5     # window sill height (windows are cut slightly into the ring)
RING_T = 4.6        # base ring wall thickness
SHELL_T = 1.6       # dome shell thickness
TOP_HOLE_R = 19.6   # top opening radius
WIN_HALF = 24.2     # half width of the four side windows
WIN_TOP = 41.8      # window head height
BAR_HALF = 15.8     # half width of the bottom cross bar
BAR_T = 4.2         # cross bar thickness

# snap clip (one on +Y side, a copy rotated 180 deg on -Y side)
ROOT_X0, ROOT_X1 = -10.3, 0.0     # root block x-range
ROOT_Y0, ROOT_Y1 = 34.2, 35.6     # inner (flat) face y at ROOT_X0 / ROOT_X1
ROOT_H = 15.0                     # root block height
ROOT_GW, ROOT_GH = 1.4, 4.0       # steep relief chamfer where root meets the ring
ARM_R_IN, ARM_R_OUT = 36.3, 42.4  # cantilever arm radii
ARM_X1 = 12.6                     # arm tip (flat end face x)
ARM_H = 9.4                       # arm height
CH_W, CH_H = 3.3, 4.0             # chamfer on the arm outer top edge (radial, vertical)

RI = R - SHELL_T
R_IN = R - RING_T

# ---------------- base ring ----------------
ring = cq.Workplane("XY").circle(R).circle(R_IN).extrude(H_RING)

# ---------------- dome shell ----------------
# Solid spheres built with their poles on the X axis and their parametric seam under the
# equator, so the kept upper hemisphere shell is seam-free.
def sphere_x(r):
    s_ = cq.Solid.makeSphere(r, angleDegrees1=-90, angleDegrees2=90)
    return cq.Workplane("XY").add(s_.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90))


upper = cq.Workplane("XY").box(3 * R, 3 * R, 2 * R, centered=(True, True, False))
hole = (
    cq.Workplane("XY")
    .circle(TOP_HOLE_R)
    .extrude(2 * R)
    .rotate((0, 0, 0), (0, 0, 1), -45)      # seam of the hole wall faces away from the main view
)
dome = (
    sphere_x(R)
    .cut(sphere_x(RI))
    .intersect(upper)
    .cut(hole)
    .translate((0, 0, H_RING))
)

# base ring seam turned to +Y, where it coincides with the clip root edge
body = ring.rotate((0, 0, 0), (0, 0, 1), 90).union(dome)

# ---------------- four side windows (two crossing box cuts) ----------------
L = 3 * R
WIN_H = WIN_TOP - WIN_SILL
win_x = cq.Workplane("XY").box(L, 2 * WIN_HALF, WIN_H, centered=(True, True, False)).translate((0, 0, WIN_SILL))
win_y = cq.Workplane("XY").box(2 * WIN_HALF, L, WIN_H, centered=(True, True, False)).translate((0, 0, WIN_SILL))
body = body.cut(win_x).cut(win_y)

# ---------------- bottom cross bar ----------------
bar = (
    cq.Workplane("XY")
    .box(2 * R_IN + 2, 2 * BAR_HALF, BAR_T, centered=(True, True, False))
    .intersect(cq.Workplane("XY").circle(R_IN + 0.5).extrude(BAR_T))
)
body = body.union(bar)


# ---------------- snap clips ----------------
def chamfer_ring(r_top, z_top_, w, h):
    """revolved cutter removing a conical chamfer band out to (beyond) the ring bore"""
    return (
        cq.Workplane("XZ")
        .polyline([(r_top, z_top_ + 0.5), (r_top, z_top_), (r_top + w, z_top_ - h),
                   (R_IN + 0.5, z_top_ - h), (R_IN + 0.5, z_top_ + 0.5)])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )


def make_clip():
    # root block: flat inner face, merges into the ring wall
    root = (
        cq.Workplane("XY")
        .polyline([(ROOT_X0, ROOT_Y0), (ROOT_X1, ROOT_Y1), (ROOT_X1, R - 1.0), (ROOT_X0, R - 2.0)])
        .close()
        .extrude(ROOT_H)
        .intersect(cq.Workplane("XY").circle(R_IN + 0.3).extrude(ROOT_H))
    )
    root = root.cut(chamfer_ring(R_IN - ROOT_GW, ROOT_H, ROOT_GW, ROOT_GH))
    # curved cantilever arm, chamfered outer top edge, free of the ring (slot)
    arm = (
        cq.Workplane("XY")
        .circle(ARM_R_OUT)
        .circle(ARM_R_IN)
        .extrude(ARM_H)
        .intersect(
            cq.Workplane("XY")
            .box(ARM_X1 - ROOT_X1 + 0.3, R, ARM_H, centered=False)
            .translate((ROOT_X1 - 0.3, 0, 0))
        )
    )
    arm = arm.cut(chamfer_ring(ARM_R_OUT - CH_W, ARM_H, CH_W + 0.01, CH_H))
    return root.union(arm)


clip = make_clip()
body = body.union(clip).union(clip.rotate((0, 0, 0), (0, 0, 1), 180))

result = body
